import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 59.0          # cup outer radius
H_CUP = 35.3          # cup height (z = 0 .. H_CUP)
WALL = 4.3            # cup wall thickness
FLOOR_Z = 5.0         # top of cup floor
RIB_R = 2.45          # inner vertical rib radius (two ribs at +/-X)
RIB_INSET = 0.25      # rib axis sits this far inside the bore surface

R_BOSS = 41.25        # lower boss radius
H_BOSS = 21.8         # lower boss height (z = -H_BOSS .. 0)
FLAT_Y = 36.0         # distance of boss flat (faces -Y) from axis

SOCK_A = 29.0         # socket square half side
SOCK_DEPTH = 23.0     # socket depth from boss bottom face
PIN_R = 4.37          # corner pin radius
PIN_OFF = 5.41        # pin centre distance from square corner (along diagonal)
BUMP_R = 14.8         # mid-side bump radius
BUMP_SAG = 3.7        # mid-side bump protrusion into socket

R_IN = R_OUT - WALL


def cyl(x, y, z0, r, h, ang_deg=0.0):
    """Vertical cylinder; ang_deg sets where the seam edge lies."""
    a = math.radians(ang_deg)
    pl = cq.Plane(origin=(x, y, z0), xDir=(math.cos(a), math.sin(a), 0),
                  normal=(0, 0, 1))
    return cq.Workplane(pl).circle(r).extrude(h)


# ---------------- cup ----------------
cup = cyl(0, 0, 0, R_OUT, H_CUP, 90)
pocket = cyl(0, 0, FLOOR_Z, R_IN, H_CUP - FLOOR_Z + 1.0, 0)
for sx in (1, -1):
    rib = cyl(sx * (R_IN - RIB_INSET), 0, FLOOR_Z - 1.0, RIB_R, H_CUP - FLOOR_Z + 3.0,
              0 if sx > 0 else 180)
    pocket = pocket.cut(rib)
cup = cup.cut(pocket)

# ---------------- boss with flat ----------------
boss = cyl(0, 0, -H_BOSS, R_BOSS, H_BOSS + 0.5, -90)
flat_cut = (cq.Workplane("XY").workplane(offset=-H_BOSS - 1)
            .center(0, -FLAT_Y - 50).rect(200, 100).extrude(H_BOSS + 1))
boss = boss.cut(flat_cut)

body = cup.union(boss)

# ---------------- socket in boss ----------------
z0 = -H_BOSS - 1.0
sock_h = SOCK_DEPTH + 1.0
sock = (cq.Workplane("XY").workplane(offset=z0)
        .rect(2 * SOCK_A, 2 * SOCK_A).extrude(sock_h))

s2 = math.sqrt(2.0)
t = PIN_OFF / s2
for sx, sy in ((1, 1), (-1, 1), (-1, -1), (1, -1)):
    kx, ky = sx * SOCK_A, sy * SOCK_A                 # square corner
    cx, cy = kx - sx * t, ky - sy * t                 # pin centre
    ang = math.degrees(math.atan2(sy, sx))
    pin = cyl(cx, cy, z0 - 1, PIN_R, sock_h + 2, ang)
    # keep the small sliver between the pin and the square corner solid
    corner_fill = (cq.Workplane("XY").workplane(offset=z0 - 1)
                   .polyline([(kx + sx, ky + sy), (cx, ky + sy), (cx, cy), (kx + sx, cy)])
                   .close().extrude(sock_h + 2))
    sock = sock.cut(pin).cut(corner_fill)

e = SOCK_A - BUMP_SAG + BUMP_R
for ang in (0, 90, 180, 270):
    a = math.radians(ang)
    bump = cyl(e * math.cos(a), e * math.sin(a), z0 - 1, BUMP_R, sock_h + 2, ang)
    sock = sock.cut(bump)

result = body.cut(sock)

VIEW = {"azimuth": 45, "elevation": 26}
